import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_W = 474.0        # overall width (X)
PLATE_H = 360.0        # overall height (Z)
PLATE_T = 6.5          # plate thickness (Y)
EAR_W = 32.0           # width of the corner ears
NOTCH_D = 51.0         # depth of top / bottom notch between the ears
NOTCH_R = 33.0         # fillet radius at the notch root
EAR_R = 8.0            # corner radius at the ear tips

BAR_L = 419.0          # rail length (X)
BAR_H = 12.7           # rail height (Z)
BAR_P = 6.8            # rail protrusion from front face (-Y)
BAR_Z = [64.6, -9.0, -92.3]   # rail centre heights

HOLE_D = 6.6

HOLES = [
    (-225.1, 163.7), (224.9, 163.7), (-225.1, -164.3), (224.9, -164.3),
    (-204.9, 104.3), (-97.9, 102.9), (151.5, 112.7), (106.1, 80.9),
    (197.1, 80.9), (-204.9, 11.7), (-97.9, 5.5), (-61.7, 5.5),
    (-217.9, -25.1), (-169.7, -25.1), (106.1, -23.7), (197.1, -23.7),
    (4.1, -36.3), (97.7, -36.3), (151.5, -69.9), (-145.5, -78.9),
    (-53.3, -78.9), (-217.9, -106.9), (-169.7, -106.9), (-145.5, -120.5),
    (-53.3, -120.5), (4.1, -114.7), (97.7, -114.7),
]

# ---------------- plate outline (in XZ plane) ----------------
hw, hh = PLATE_W / 2.0, PLATE_H / 2.0
ix = hw - EAR_W          # inner x of the ears
iz = hh - NOTCH_D        # z of the notch bottom

pts = [
    (-hw, -hh), (-ix, -hh), (-ix, -iz), (ix, -iz), (ix, -hh), (hw, -hh),
    (hw, hh), (ix, hh), (ix, iz), (-ix, iz), (-ix, hh), (-hw, hh),
]

# Workplane "XZ": local x -> +X, local y -> +Z, normal -> -Y
plate = (
    cq.Workplane("XZ")
    .polyline(pts).close()
    .extrude(-PLATE_T)          # extrude toward +Y
)

# round the outer ear corners and the notch roots (edges parallel to Y)
plate = plate.edges("|Y").edges(
    cq.selectors.BoxSelector((-ix - 1, -50, -iz - 1), (ix + 1, 50, iz + 1))
).fillet(NOTCH_R)
plate = plate.edges("|Y").fillet(EAR_R)

# holes through the plate
cutters = (
    cq.Workplane("XZ", origin=(0, -1.0, 0))
    .pushPoints(HOLES)
    .circle(HOLE_D / 2.0)
    .extrude(-(PLATE_T + 2.0))   # toward +Y, through the plate
)
plate = plate.cut(cutters)

# rails on the front (-Y) face
for z in BAR_Z:
    bar = (
        cq.Workplane("XY")
        .box(BAR_L, BAR_P, BAR_H)
        .translate((0, -BAR_P / 2.0, z))
    )
    plate = plate.union(bar)

result = plate
VIEW = {"azimuth": 45, "elevation": 26}
